import math
import cadquery as cq

# =====================================================================
#  Wall-mount holder / tray: U shaped shell (front, two sides, bottom),
#  open at the back and at the top, with a double front wall, four grip
#  pads on the front, a window, hinge knuckles and screw bosses.
#  X = width, Y = depth (front face at Y=0, open back at Y=D), Z = height
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 53.6          # overall width (X) of the shell
D = 29.8          # body depth (Y)
H = 100.0         # overall height (Z)

T_SIDE = 2.6      # side wall thickness (behind the front cavity)
T_SIDE_CAV = 1.35 # side wall thickness beside the front cavity
T_FRONT = 1.25    # outer front skin thickness
CAV_DEPTH = 6.95  # depth (Y) of the open-top cavity behind the front skin
T_INNER = 1.2     # inner wall between cavity and main compartment
INNER_DROP = 2.3  # the inner wall stops this much below the top
T_BOT = 3.0       # bottom wall thickness
GROOVE_W = 1.0    # guide groove width (Y) behind the inner wall
CAV_FLOOR = 9.3   # floor level of the cavity behind the front skin
LATCH_W, LATCH_T, LATCH_H = 13.6, 1.2, 3.4   # snap ramp inside the cavity

# front window
WIN_W, WIN_Z0, WIN_Z1, WIN_CH, WIN_R = 13.6, 4.8, 23.6, 2.2, 1.0

# grip pads (four, at the corners of the front face)
PAD_H = 3.6       # how far the pads stand proud of the front face
PAD_BASE_X = 10.0 # |X| where the pad flank meets the front face
PAD_R_IN = 1.25   # concave blend at the foot of the flank
PAD_R_OUT = 1.8   # convex round at the front of the flank
PAD_OVERSHOOT = 0.35
# side profile of the top pad (distances measured down from the top):
# a straight lead-in at TP_ANG from vertical, blended by a TP_R arc into
# the flat pad face, which runs back into the front face by an S curve
# between TP_FLAT and TP_END
TP_ANG, TP_R, TP_FLAT, TP_END = 27.5, 10.0, 18.4, 29.9
# the same for the bottom pad (distances measured up from the bottom)
BP_ANG, BP_R, BP_FLAT, BP_END = 24.0, 9.0, 19.0, 30.2

# small rectangular pockets (pad flanks and side faces), from the ends
SLOT_Z0, SLOT_Z1 = 8.1, 20.2
FLANK_NOTCH = 0.1
SIDE_POCKET_DEPTH = 0.8
SIDE_POCKET_Y0, SIDE_POCKET_Y1 = -2.45, 0.3

# screw bosses on top of the side walls, hinge knuckles at the back
BOSS_D, BOSS_L, BOSS_HOLE, BOSS_Y = 4.9, 6.1, 2.1, 14.8
KN_D, KN_L, KN_HOLE = 4.9, 5.9, 1.6
KN_TOP_Z = H - 3.67            # axis height of the upper knuckles
KN_BOT_Z = 2.5                 # axis height of the lower knuckles

# derived
X_IN = W / 2 - T_SIDE
X_CAV = W / 2 - T_SIDE_CAV
Y_CAV0 = T_FRONT
Y_CAV1 = T_FRONT + CAV_DEPTH
Y_MAIN0 = Y_CAV1 + T_INNER
X_WALL = W / 2 - T_SIDE / 2     # side wall mid-plane


def smooth_curve(plane, pts, tgs):
    """One smooth spline edge through the key points of a tangent chain of
    lines and arcs (with their exact tangents), so that the swept surface
    is a single face.  Deviation from the line/arc chain is < 0.01 mm."""
    return cq.Edge.makeSpline([plane.toWorldCoords(p) for p in pts],
                              tangents=[plane.toWorldCoords(t) -
                                        plane.toWorldCoords((0, 0))
                                        for t in tgs],
                              scale=True)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------- main U shaped shell ----------------
body = box(-W / 2, W / 2, 0, D, 0, H)
# main compartment (open back and open top)
body = body.cut(box(-X_IN, X_IN, Y_MAIN0, D + 1, T_BOT, H + 1))
# cavity between front skin and inner wall (open top)
body = body.cut(box(-X_CAV, X_CAV, Y_CAV0, Y_CAV1, CAV_FLOOR, H + 1))
# the inner wall is a little lower than the rest of the rim
body = body.cut(box(-X_IN, X_IN, Y_CAV1 - 0.01, Y_MAIN0 + 0.01,
                    H - INNER_DROP, H + 1))
# vertical guide grooves in the side walls just behind the inner wall
body = body.cut(box(-X_CAV, X_CAV, Y_MAIN0, Y_MAIN0 + GROOVE_W, T_BOT, H + 1))
# deeper well behind the window, down to the window sill, rounded bottom
well = box(-WIN_W / 2, WIN_W / 2, -1.0, Y_CAV1, WIN_Z0, CAV_FLOOR + 1.0)
well = well.edges("<Z and (|Y or >Y)").fillet(WIN_R)
body = body.cut(well)
# snap ramp on the inside of the front skin, at the top of the cavity
latch = (cq.Workplane("YZ", origin=(-LATCH_W / 2, 0, 0))
         .polyline([(Y_CAV0 - 0.1, H), (Y_CAV0, H),
                    (Y_CAV0 + LATCH_T, H - LATCH_H),
                    (Y_CAV0 - 0.1, H - LATCH_H)]).close()
         .extrude(LATCH_W))
body = body.union(latch)


# ---------------- grip pads ----------------
def pad_side_solid(top):
    """Side profile (Y,Z) of one pad: straight lead-in from the rim,
    tangent arc into the flat face, tangent S curve back into the front
    face.  Extruded across the whole width, trimmed later."""
    P = PAD_H
    if top:
        z0, sg, ang, r, flat, end = H, -1.0, TP_ANG, TP_R, TP_FLAT, TP_END
    else:
        z0, sg, ang, r, flat, end = 0.0, 1.0, BP_ANG, BP_R, BP_FLAT, BP_END
    a = math.radians(ang)
    lead = (P - r * (1.0 - math.cos(a))) / math.sin(a)
    ramp = lead * math.cos(a) + r * math.sin(a)
    p0 = (0.0, z0)                                           # rim edge
    p1 = (-lead * math.sin(a), z0 + sg * lead * math.cos(a))  # end of lead
    p2 = (-P, z0 + sg * ramp)                                # on pad face
    p3 = (-P, z0 + sg * flat)                                # S curve start
    p4 = (-P / 2.0, z0 + sg * (flat + end) / 2.0)            # S inflexion
    p5 = (0.0, z0 + sg * end)                                # back on front
    # mid point of the corner arc (centre at (-P + r, p2.z))
    pa = (-P + r - r * math.cos(a / 2), p2[1] - sg * r * math.sin(a / 2))
    # the S curve is two equal tangent arcs
    dz = end - flat
    rs = (P * P + dz * dz) / (4.0 * P)
    phi = math.asin(min(1.0, (dz / 2.0) / rs))
    q1 = (-P + rs - rs * math.cos(phi / 2), p3[1] + sg * rs * math.sin(phi / 2))
    q2 = (-rs + rs * math.cos(phi / 2), p5[1] - sg * rs * math.sin(phi / 2))
    t_lead = (-math.sin(a), sg * math.cos(a))
    t_mid = (math.sin(phi / 2), sg * math.cos(phi / 2))
    pl = cq.Plane(origin=(-W / 2 - 1, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0))
    curve = smooth_curve(
        pl,
        [p0, p1, pa, p2, p3, q1, p4, q2, p5],
        [t_lead, t_lead, (-math.sin(a / 2), sg * math.cos(a / 2)), (0, sg),
         (0, sg), t_mid, (math.sin(phi), sg * math.cos(phi)), t_mid, (0, sg)])
    g = lambda y, z: pl.toWorldCoords((y, z))
    back = [cq.Edge.makeLine(g(*p5), g(0.6, p5[1])),
            cq.Edge.makeLine(g(0.6, p5[1]), g(0.6, z0)),
            cq.Edge.makeLine(g(0.6, z0), g(0.0, z0))]
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges([curve] + back))
    return cq.Workplane(pl).add(cq.Solid.extrudeLinear(face, cq.Vector(W + 2, 0, 0)))


def pad_footprint(side):
    """Plan (XY) shape of one pad column: blended, rounded inner flank.
    The front round overshoots the pad face slightly so that the side
    profile (not this footprint) defines the pad front."""
    s = side
    P = PAD_H + PAD_OVERSHOOT
    xb = s * PAD_BASE_X                   # flank foot on the front face
    xf = xb + s * PAD_R_IN                # flank line
    xo = xf + s * PAD_R_OUT               # where the front round ends
    c45 = math.sqrt(0.5)
    pl = cq.Plane(origin=(0, 0, -1), xDir=(1, 0, 0), normal=(0, 0, 1))
    t45 = (s * c45, -c45)
    curve = smooth_curve(
        pl,
        [(xb, 0.0),
         (xb + s * PAD_R_IN * c45, -PAD_R_IN * (1 - c45)),
         (xf, -PAD_R_IN),
         (xf, -(P - PAD_R_OUT)),
         (xf + s * PAD_R_OUT * (1 - c45), -(P - PAD_R_OUT) - PAD_R_OUT * c45),
         (xo, -P)],
        [(s, 0.0), t45, (0.0, -1.0), (0.0, -1.0), t45, (s, 0.0)])
    g = lambda x, y: pl.toWorldCoords((x, y))
    xe = s * (W / 2 + 2)
    pts = [(xo, -P), (xo - s * 0.01, -P - 1.0), (xe, -P - 1.0), (xe, 0.8),
           (xb, 0.8), (xb, 0.0)]
    edges = [curve] + [cq.Edge.makeLine(g(*a), g(*b))
                       for a, b in zip(pts[:-1], pts[1:])]
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Workplane(pl).add(
        cq.Solid.extrudeLinear(face, cq.Vector(0, 0, H + 2)))


for s in (-1, 1):
    foot = pad_footprint(s)
    for top in (True, False):
        p = pad_side_solid(top).intersect(foot)
        p = p.intersect(box(-W / 2, W / 2, -PAD_H - 1, 1.0, -1, H + 1))
        body = body.union(p)

# ---------------- front window ----------------
win = (cq.Workplane("XZ", origin=(0, 0, 0))
       .center(0, (WIN_Z0 + WIN_Z1) / 2)
       .rect(WIN_W, WIN_Z1 - WIN_Z0)
       .extrude(-(T_FRONT + 0.5))
       .translate((0, -0.2, 0)))
win = win.edges("|Y and >Z").chamfer(WIN_CH)
win = win.edges("|Y and <Z").fillet(WIN_R)
body = body.cut(win)

# ---------------- small pockets ----------------
for zc0, zc1 in ((SLOT_Z0, SLOT_Z1), (H - SLOT_Z1, H - SLOT_Z0)):
    for s in (-1, 1):
        # notch in the inner flank of each pad (removes the foot blend)
        xa, xb = sorted((s * (PAD_BASE_X + PAD_R_IN + FLANK_NOTCH),
                         s * (PAD_BASE_X - 0.3)))
        body = body.cut(box(xa, xb, -PAD_R_IN - 0.2, 0.0, zc0, zc1))
        # pocket in the side face close to the front
        xo = s * W / 2
        xa, xb = sorted((xo, xo - s * SIDE_POCKET_DEPTH))
        body = body.cut(box(xa - (0.5 if s < 0 else 0),
                            xb + (0.5 if s > 0 else 0),
                            SIDE_POCKET_Y0, SIDE_POCKET_Y1, zc0, zc1))

# ---------------- vertical screw bosses at top of side walls ----------------
for s in (-1, 1):
    b = (cq.Workplane("XY", origin=(s * X_WALL, BOSS_Y, H - BOSS_L))
         .circle(BOSS_D / 2).extrude(BOSS_L))
    b = b.faces("<Z").edges().fillet(1.2)
    body = body.union(b)
    body = body.cut(cq.Workplane("XY", origin=(s * X_WALL, BOSS_Y, H - 5.0))
                    .circle(BOSS_HOLE / 2).extrude(6))

# ---------------- hinge knuckles at the back corners ----------------
for s in (-1, 1):
    for zc in (KN_TOP_Z, KN_BOT_Z):
        k = (cq.Workplane("XZ", origin=(s * X_WALL, D, zc))
             .circle(KN_D / 2).extrude(KN_L))
        k = k.faces("<Y").edges().fillet(1.6)
        body = body.union(k)
        body = body.cut(cq.Workplane("XZ", origin=(s * X_WALL, D + 0.1, zc))
                        .circle(KN_HOLE / 2).extrude(KN_L - 1.5))

# ---------------- floor details ----------------
# obround recess with two through holes near the +X wall
OB_X, OB_Y0, OB_Y1, OB_W, OB_DEPTH = 20.33, 12.35, 25.35, 6.7, 0.7
HOLE_X, HOLE_YS, HOLE_D = 20.5, (15.1, 22.2), 4.4
ob = (cq.Workplane("XY", origin=(OB_X, (OB_Y0 + OB_Y1) / 2, T_BOT - OB_DEPTH))
      .slot2D(OB_Y1 - OB_Y0, OB_W, angle=90).extrude(2))
body = body.cut(ob)
for yc in HOLE_YS:
    body = body.cut(cq.Workplane("XY", origin=(HOLE_X, yc, -1))
                    .circle(HOLE_D / 2).extrude(T_BOT + 2))

# low rectangular rim around a through slot near the -X back corner
body = body.union(box(-23.85, -17.0, 21.3, 24.8, T_BOT - 0.1, T_BOT + 0.6))
body = body.cut(box(-22.25, -18.4, 22.1, 23.9, -1, T_BOT + 2))

# L shaped rib standing against the inner wall
RIB_X0, RIB_X1, RIB_Y0, RIB_Y1 = 13.4, 16.4, 6.0, 17.1
body = body.union(box(RIB_X0, RIB_X1, RIB_Y0, Y_MAIN0 + 1.2,
                      T_BOT - 0.1, T_BOT + 11))
body = body.union(box(RIB_X0, RIB_X1, RIB_Y0, RIB_Y1,
                      T_BOT - 0.1, T_BOT + 1.2))

# shallow rectangular recess under the bottom
body = body.cut(box(-12.2, 13.5, 1.8, 27.0, -1, 0.5))

result = body

VIEW = {"azimuth": 45, "elevation": 26}
